import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
FLANGE_R = 60.0        # upper flange radius
SPIGOT_R = 56.7        # lower spigot ring radius
SPIGOT_H = 4.85         # spigot thickness (z 0..SPIGOT_H)
FLANGE_TOP = 9.7      # top of flange
FLANGE_CH = 0.8        # chamfer on the flange / spigot outer edges
BODY_R = 50.3          # main body radius
TOP_Z = 48.0           # overall height
TOP_CH = 0.8           # chamfer on the top outer edge

GROOVE_R = 7.9        # screw-head clearance grooves (centred on flange holes)
GROOVE_FILLET = 3.0
FL_HOLE_ANG = 30.6     # flange holes at +-ANG about the X axis, both sides
GROOVE_ANGLES = [FL_HOLE_ANG, 180 - FL_HOLE_ANG, 180 + FL_HOLE_ANG, 360 - FL_HOLE_ANG]
FL_HOLE_D = 8.3        # flange holes
FL_HOLE_PCR = 50.6

BORE_D = 50.6          # central blind bore in the top
BORE_DEPTH = 10.8
BORE_CH = 0.8

TOP_HOLE_PCR = 40.0
TOP_HOLE_D = 8.0
TOP_HOLE_DEPTH = 12.0
TOP_CB_D = 10.2
TOP_CB_DEPTH = 1.2
TOP_HOLE_ANGLES = [45, 135, 225, 315]
BIG_HOLE_D = 10.5      # single blind hole at +X
BIG_HOLE_DEPTH = 12.0

PIN_HOLE_R = 49.0      # blind hole in the underside at +X
PIN_HOLE_D = 7.0
PIN_HOLE_DEPTH = 8.0

CAV_R = 40.0           # inner cavity radius
CEIL_Z = 31.5          # cavity ceiling
CEIL_REC_R = 32.5      # shallow circular recess in the ceiling
CEIL_REC_D = 1.0
FRONT_POCKET_HW = 31.5  # full-height pocket toward -Y behind the obround slot
FRONT_POCKET_R = 48.0
BACK_POCKET_HW = 21.0   # shallow pocket in the underside under the +Y window
BACK_POCKET_R = 47.5
BACK_POCKET_H = 5.0
BACK_FLAT_Y = 43.0      # full-height flat-walled pocket behind the +Y window
SIDE_POCKET_HW = 14.0   # shallow pocket in the underside toward -X
SIDE_POCKET_R = 52.0
SIDE_POCKET_H = 4.0
POCKET_FILLET = 2.5      # corner radius of the milled pockets
RIB_PCR = 40.5          # vertical rib on the cavity wall next to the -X pocket
RIB_ANGLE = 168.5
RIB_R = 4.5
RIB_TOP = 26.5
RIB_FILLET = 2.0

SLOT_L = 48.0          # front (-Y) obround slot
SLOT_H = 16.0
SLOT_ZC = 20.5
WIN_W = 43.0           # back (+Y) rectangular window
WIN_Z1 = 30.0
WIN_CR_TOP = 4.0
WIN_CR_BOT = 3.0


def polar(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


def pocket(cx, cy, w, h, r, height):
    """Rectangle (centre cx,cy, size w x h) clipped by a circle of radius r about
    the axis, corners rounded by the cutter radius, extruded from just below z=0."""
    sk = (cq.Sketch()
          .push([(cx, cy)]).rect(w, h)
          .reset().circle(r, mode="i")
          .reset().vertices().fillet(POCKET_FILLET))
    return cq.Workplane("XY").workplane(offset=-1).placeSketch(sk).extrude(height)


groove_pts = [polar(FL_HOLE_PCR, a) for a in GROOVE_ANGLES]

# ---------------- flange + spigot (stacked discs with chamfered outer edges) ----------------
flange = (cq.Workplane("XY").circle(SPIGOT_R).extrude(SPIGOT_H)
          .faces("<Z").edges().chamfer(FLANGE_CH))
upper = (cq.Workplane("XY").workplane(offset=SPIGOT_H)
         .circle(FLANGE_R).extrude(FLANGE_TOP - SPIGOT_H)
         .faces(">Z").edges().chamfer(FLANGE_CH))
flange = flange.union(upper)

# ---------------- body: circle with four filleted screw-head grooves ----------------
body_sk = (cq.Sketch()
           .circle(BODY_R)
           .push(groove_pts).circle(GROOVE_R, mode="s")
           .reset().vertices().fillet(GROOVE_FILLET))
body_outline = (cq.Workplane("XY").workplane(offset=FLANGE_TOP - 1)
                .placeSketch(body_sk).extrude(TOP_Z - FLANGE_TOP + 2))
# plain cylinder with the chamfered top rim, then the grooves are cut through it
body = (cq.Workplane("XY").workplane(offset=FLANGE_TOP).circle(BODY_R)
        .extrude(TOP_Z - FLANGE_TOP).faces(">Z").edges().chamfer(TOP_CH))
groove_cutter = (cq.Workplane("XY").workplane(offset=FLANGE_TOP - 1)
                 .circle(BODY_R + 2).extrude(TOP_Z - FLANGE_TOP + 2)
                 .cut(body_outline))
body = body.cut(groove_cutter)

part = flange.union(body)

# ---------------- inner cavity, open at the bottom ----------------
H = CEIL_Z + 1
cav = cq.Workplane("XY").workplane(offset=-1).circle(CAV_R).extrude(H)
fp = pocket(0, -(FRONT_POCKET_R + 5) / 2, 2 * FRONT_POCKET_HW, FRONT_POCKET_R + 5, FRONT_POCKET_R, H)
rec = cq.Workplane("XY").workplane(offset=CEIL_Z - 0.5).circle(CEIL_REC_R).extrude(CEIL_REC_D + 0.5)
part = part.cut(cav).cut(fp).cut(rec)

bp = pocket(0, (BACK_POCKET_R + 5) / 2, 2 * BACK_POCKET_HW, BACK_POCKET_R + 5, BACK_POCKET_R, BACK_POCKET_H + 1)
sp = pocket(-(SIDE_POCKET_R + 5) / 2, 0, SIDE_POCKET_R + 5, 2 * SIDE_POCKET_HW, SIDE_POCKET_R, SIDE_POCKET_H + 1)
bf = (cq.Workplane("XY").workplane(offset=-1).center(0, BACK_FLAT_Y / 2)
      .rect(WIN_W, BACK_FLAT_Y).extrude(H + CEIL_REC_D))
part = part.cut(bp).cut(sp).cut(bf)

rib = (cq.Workplane("XY").workplane(offset=SIDE_POCKET_H).center(*polar(RIB_PCR, RIB_ANGLE))
       .circle(RIB_R).extrude(RIB_TOP - SIDE_POCKET_H)
       .faces(">Z").edges().fillet(RIB_FILLET))
part = part.union(rib)

# ---------------- central blind bore with an edge chamfer ----------------
bore = (cq.Workplane("XY").workplane(offset=TOP_Z - BORE_DEPTH)
        .circle(BORE_D / 2).extrude(BORE_DEPTH + 1))
bore_ch = (cq.Workplane("XY").workplane(offset=TOP_Z - BORE_CH)
           .circle(BORE_D / 2).workplane(offset=BORE_CH + 0.01)
           .circle(BORE_D / 2 + BORE_CH + 0.01).loft())
part = part.cut(bore).cut(bore_ch)

# ---------------- flange holes ----------------
fl_holes = (cq.Workplane("XY").workplane(offset=-1).pushPoints(groove_pts)
            .circle(FL_HOLE_D / 2).extrude(FLANGE_TOP + 2))
part = part.cut(fl_holes)

# ---------------- top holes (spot-faced, blind) ----------------
tp = [polar(TOP_HOLE_PCR, a) for a in TOP_HOLE_ANGLES]
th = (cq.Workplane("XY").workplane(offset=TOP_Z - TOP_HOLE_DEPTH).pushPoints(tp)
      .circle(TOP_HOLE_D / 2).extrude(TOP_HOLE_DEPTH + 1))
tcb = (cq.Workplane("XY").workplane(offset=TOP_Z - TOP_CB_DEPTH).pushPoints(tp)
       .circle(TOP_CB_D / 2).extrude(TOP_CB_DEPTH + 1))
bh = (cq.Workplane("XY").workplane(offset=TOP_Z - BIG_HOLE_DEPTH).center(TOP_HOLE_PCR, 0)
      .circle(BIG_HOLE_D / 2).extrude(BIG_HOLE_DEPTH + 1))
ph = (cq.Workplane("XY").workplane(offset=-1).center(PIN_HOLE_R, 0)
      .circle(PIN_HOLE_D / 2).extrude(PIN_HOLE_DEPTH + 1))
part = part.cut(th).cut(tcb).cut(bh).cut(ph)

# ---------------- front obround slot (-Y) ----------------
slot = (cq.Workplane("XZ").center(0, SLOT_ZC).slot2D(SLOT_L, SLOT_H)
        .extrude(BODY_R + 5))
part = part.cut(slot)

# ---------------- back rectangular window (+Y), bottom flush with the flange top ----
win = (cq.Workplane("XZ").center(0, (FLANGE_TOP + WIN_Z1) / 2)
       .rect(WIN_W, WIN_Z1 - FLANGE_TOP).extrude(-(BODY_R + 5)))
win = win.edges("|Y and >Z").fillet(WIN_CR_TOP)
win = win.edges("|Y and <Z").fillet(WIN_CR_BOT)
part = part.cut(win)

result = part
